import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_BAND_BOT = 30.0      # radius of the grip band at its lower outer edge (max radius)
Z_BAND_BOT = 6.32      # height of the band's lower outer edge
H_TOP = 25.4           # height of the dome apex (band sphere apex)
Z_LEDGE = 14.95        # height of the small ledge (groove floor) between dome and band
GROOVE_H = 0.4         # height of the small groove separating dome and band
GROOVE_D = 0.4         # radial depth of that groove
T_DOME = 0.15          # dome sphere sits this much inside the band sphere
CHAMFER = 0.6          # chamfer under the band outer edge
R_SKIRT = 25.3         # skirt root radius
Z_UNDER = Z_BAND_BOT - CHAMFER   # flat underside of band
WALL = 0.9             # skirt wall thickness at the rim
RIM_STEP = 0.6         # short cylindrical bore above the rim
CAV_APEX = 23.6        # height of the apex of the spherical inner cavity

# thread
PITCH = 2.5
THREAD_DEPTH = 1.0
THREAD_BASE_W = 2.3
THREAD_TOP_W = 0.3
THREAD_TOP_Z = 4.6     # crest height of the upper thread end (at +X)
THREAD_TURNS = 2.5
THREAD_END_ANGLE = 0.0  # angular position of the thread's upper end (deg, CCW from +X)

# sphere through apex and band lower edge, centre on the axis
ZC = (H_TOP ** 2 - R_BAND_BOT ** 2 - Z_BAND_BOT ** 2) / (2.0 * (H_TOP - Z_BAND_BOT))
RS = H_TOP - ZC
R_IN_CYL = R_SKIRT - WALL    # inner bore radius at the rim
_d = CAV_APEX - RIM_STEP
R_CAV = (R_IN_CYL ** 2 + _d ** 2) / (2.0 * _d)   # cavity sphere radius
ZC_CAV = CAV_APEX - R_CAV


def sph_r(R, z):
    return math.sqrt(R * R - (z - ZC) ** 2)


def sph_mid(R, z0, z1):
    """point on sphere meridian halfway (in angle) between heights z0 and z1 (r>=0)."""
    a0 = math.atan2(z0 - ZC, sph_r(R, z0))
    a1 = math.atan2(z1 - ZC, sph_r(R, z1))
    am = 0.5 * (a0 + a1)
    return (R * math.cos(am), ZC + R * math.sin(am))


# ---------------- revolved body and spherical cavity ----------------
RD = RS - T_DOME             # dome sphere radius
z_db = Z_LEDGE + GROOVE_H
r_db = sph_r(RD, z_db)
r_bt = sph_r(RS, Z_LEDGE)
a0c = math.atan2(RIM_STEP - ZC_CAV, R_IN_CYL)
amc = 0.5 * (a0c + math.pi / 2)

outer = (
    cq.Workplane("XZ")
    .moveTo(0, ZC + RD)
    .threePointArc(sph_mid(RD, ZC + RD - 1e-9, z_db), (r_db, z_db))
    .lineTo(r_bt - GROOVE_D, z_db)
    .lineTo(r_bt - GROOVE_D, Z_LEDGE)
    .lineTo(r_bt, Z_LEDGE)
    .threePointArc(sph_mid(RS, Z_LEDGE, Z_BAND_BOT), (R_BAND_BOT, Z_BAND_BOT))
    .lineTo(R_BAND_BOT - CHAMFER, Z_UNDER)
    .lineTo(R_SKIRT, Z_UNDER)
    .lineTo(R_SKIRT, 0)
    .lineTo(0, 0)
    .close()
)
cavity = (
    cq.Workplane("XZ")
    .moveTo(0, -1.0)
    .lineTo(R_IN_CYL, -1.0)
    .lineTo(R_IN_CYL, RIM_STEP)
    .threePointArc((R_CAV * math.cos(amc), ZC_CAV + R_CAV * math.sin(amc)), (0, CAV_APEX))
    .close()
)
# revolve seams are turned away from the default camera (outer) and from the underside camera (cavity)
body = outer.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), 135)
body = body.cut(cavity.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), -45))

# ---------------- helical thread on the skirt ----------------
# right-hand single-start thread; its upper end sits at +X, it runs down to the rim
helix_h = PITCH * THREAD_TURNS
z0 = THREAD_TOP_Z - helix_h
ri = R_SKIRT - 0.3
ro = R_SKIRT + THREAD_DEPTH
helix = cq.Wire.makeHelix(PITCH, helix_h, ri, center=cq.Vector(0, 0, z0), dir=cq.Vector(0, 0, 1))
tprof = (
    cq.Workplane("XZ")
    .polyline([(ri, z0 - THREAD_BASE_W / 2), (ro, z0 - THREAD_TOP_W / 2),
               (ro, z0 + THREAD_TOP_W / 2), (ri, z0 + THREAD_BASE_W / 2)])
    .close()
)
thread = tprof.sweep(cq.Workplane().add(helix), isFrenet=True)
# turn the thread so that its upper end lies at THREAD_END_ANGLE
thread = thread.rotate((0, 0, 0), (0, 0, 1), THREAD_END_ANGLE - (THREAD_TURNS * 360.0) % 360.0)
clip = cq.Workplane("XY").box(100, 100, Z_UNDER, centered=(True, True, False))
thread = thread.intersect(clip)
body = body.union(thread)

# ---------------- grip band pockets and notches ----------------
# Each feature is recessed into the band sphere with a floor that follows the sphere (offset inward by depth).
# Every recess runs through the full band height (opens into the ledge and the band's lower edge).
# (start angle, end angle, depth); angles in degrees CCW from +X seen from above
PANEL_D = 0.15    # shallow panels
NOTCH_D = 1.0     # wide notches
GROOVE_DEPTH = 0.6  # narrow grooves between panels
FEATURES = [
    # shallow panels
    (-79.0, -54.0, 0.30),
    (-52.5, -42.0, PANEL_D),
    (-40.5, -30.5, PANEL_D),
    (-25.5, 5.5, PANEL_D),
    (10.5, 27.5, PANEL_D),
    (92.5, 110.5, PANEL_D),
    (111.5, 139.0, PANEL_D),
    (140.0, 153.5, PANEL_D),
    (159.5, 163.0, PANEL_D),
    (235.0, 244.8, 0.40),
    (245.6, 279.0, 0.20),
    # wide notches
    (-30.0, -26.0, NOTCH_D),
    (6.0, 10.0, NOTCH_D),
    (28.0, 34.0, NOTCH_D),
    (88.25, 91.75, NOTCH_D),
    (154.0, 159.0, NOTCH_D),
    (202.0, 208.0, NOTCH_D),
    # narrow grooves
    (110.5, 111.5, GROOVE_DEPTH),
    (139.0, 140.0, GROOVE_DEPTH),
    (279.0, 281.0, GROOVE_DEPTH),
    (-54.0, -52.5, GROOVE_DEPTH),
]
R_OUT = 45.0


def recess(a0, a1, depth):
    z1, z2 = Z_UNDER - 0.5, Z_LEDGE
    rf = RS - depth
    p1 = (sph_r(rf, z1), z1)
    p2 = (sph_r(rf, z2), z2)
    sk = (
        cq.Workplane("XZ")
        .moveTo(*p1)
        .lineTo(R_OUT, z1)
        .lineTo(R_OUT, z2)
        .lineTo(*p2)
        .threePointArc(sph_mid(rf, z2, z1), p1)
        .close()
    )
    s = sk.revolve(a1 - a0, (0, 0, 0), (0, 1, 0))
    return s.rotate((0, 0, 0), (0, 0, 1), a0)


cutter = None
for a0, a1, d in FEATURES:
    c = recess(a0, a1, d)
    cutter = c if cutter is None else cutter.union(c)
body = body.cut(cutter)

result = body
